import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 100.0            # plate side
T = 10.0             # plate thickness

# top grate pocket
N_GRID = 3           # 3 x 3 square openings
CELL = 11.8          # square opening size
PITCH = 15.7         # opening pitch
RIB_W = PITCH - CELL # rib width (3.9)
POCKET = N_GRID * CELL + (N_GRID - 1) * RIB_W   # pocket = grid outer size (43.2)
RIB_TOP = 4.45       # rib crest height above the underside
RIM_R = 3.4          # convex round on the pocket rim
RIB_R = 1.9          # round on the rib top edges (almost a full round)

# mounting holes (through, on the X / Y axes)
HOLE_OFF = 35.0
HOLE_D = 7.8

# underside recess under each mounting hole
UP_SIZE = 12.8       # square recess
UP_DEPTH = 7.5       # recess ceiling height (hole is T - UP_DEPTH long)
UP_CH_H = 1.9        # mouth chamfer, vertical leg
UP_CH_W = 2.4        # mouth chamfer, horizontal leg

# underside blind holes on the diagonals
BH_OFF = 37.0
BH_D = 8.0
BH_DEPTH = 6.0

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- base plate ----------------
plate = cq.Workplane("XY").box(L, L, T, centered=(True, True, False))

# top pocket down to the rib crest level
pocket = (cq.Workplane("XY").workplane(offset=RIB_TOP)
          .rect(POCKET, POCKET).extrude(T - RIB_TOP + 1))
plate = plate.cut(pocket)

# convex round on the pocket rim
rim = cq.selectors.BoxSelector((-POCKET/2 - 0.1, -POCKET/2 - 0.1, T - 0.1),
                               (POCKET/2 + 0.1, POCKET/2 + 0.1, T + 0.1))
plate = plate.edges(rim).fillet(RIM_R)

# 3 x 3 square openings through the pocket floor -> ribs remain
pts = [((i - (N_GRID - 1) / 2) * PITCH, (j - (N_GRID - 1) / 2) * PITCH)
       for i in range(N_GRID) for j in range(N_GRID)]
cells = (cq.Workplane("XY").workplane(offset=-1).pushPoints(pts)
         .rect(CELL, CELL).extrude(T + 2))
plate = plate.cut(cells)

# round the rib tops
ribs = cq.selectors.BoxSelector((-POCKET/2 + 0.05, -POCKET/2 + 0.05, RIB_TOP - 0.05),
                                (POCKET/2 - 0.05, POCKET/2 - 0.05, RIB_TOP + 0.05))
plate = plate.edges(ribs).fillet(RIB_R)

# mounting holes
mh = [(HOLE_OFF, 0), (-HOLE_OFF, 0), (0, HOLE_OFF), (0, -HOLE_OFF)]
plate = plate.cut(cq.Workplane("XY").workplane(offset=-1).pushPoints(mh)
                  .circle(HOLE_D / 2).extrude(T + 2))

# underside recesses: chamfered mouth + square pocket up to the hole
for (x, y) in mh:
    recess = (cq.Workplane("XY").center(x, y).rect(UP_SIZE, UP_SIZE)
              .extrude(UP_DEPTH))
    mouth = (cq.Workplane("XY").center(x, y)
             .rect(UP_SIZE + 2 * UP_CH_W, UP_SIZE + 2 * UP_CH_W)
             .workplane(offset=UP_CH_H).rect(UP_SIZE, UP_SIZE).loft())
    plate = plate.cut(recess.union(mouth))

# underside blind holes on the diagonals
bh = [(sx * BH_OFF, sy * BH_OFF) for sx in (-1, 1) for sy in (-1, 1)]
plate = plate.cut(cq.Workplane("XY").pushPoints(bh).circle(BH_D / 2).extrude(BH_DEPTH))

result = plate
